import math

import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
PLATE_X = 110.0        # base plate length along X
PLATE_Y = 100.0        # base plate length along Y
PLATE_T = 6.5          # base plate thickness
PLATE_R = 6.0          # plate corner radius (vertical edges)
BOT_CH = 0.8           # chamfer on plate bottom perimeter edge

FRAME_X = 68.0         # raised frame width (X); spans full Y
FRAME_H = 1.9          # frame height above plate top
FRAME_R = 4.5          # frame outer corner radius

RECESS_X = 64.0        # lid recess inside frame
RECESS_Y = 96.0
RECESS_D = 1.4         # recess depth from frame top
RECESS_R = 3.0

POCKET_X = 60.0        # main pocket
POCKET_Y = 92.0
FLOOR_T = 1.9          # floor thickness under pocket

BOSS_DX = 28.0         # corner boss centres (+/-)
BOSS_DY = 44.0
BOSS_R = 5.2
BOSS_HOLE_D = 3.8
NUT_AF = 8.0           # hex nut trap across flats (underside)
NUT_DEPTH = 2.5
NUT_ROT = 30.0         # hex rotation (deg)

HOLE_X = 46.7          # flange hole column position (+/-)
HOLE_PITCH = 25.5      # flange hole pitch along Y
HOLE_N = 4
HOLE_D = 6.7
CSK_D = 14.5           # countersink on underside
CSK_ANGLE = 100.0
TOP_CSK_D = 12.5       # shallow countersink on top face
TOP_CSK_ANGLE = 120.0

SLOT_N = 18
SLOT_PITCH = 3.85
SLOT_W = 2.0
SLOT_L = 51.4

TOP = PLATE_T + FRAME_H
LEDGE_Z = TOP - RECESS_D

# ---------------- base plate ----------------
plate = (
    cq.Workplane("XY")
    .rect(PLATE_X, PLATE_Y)
    .extrude(PLATE_T)
    .edges("|Z").fillet(PLATE_R)
)
plate = plate.faces("<Z").edges().chamfer(BOT_CH)

# ---------------- raised frame (flush with +/-Y faces) ----------------
frame = (
    cq.Workplane("XY")
    .workplane(offset=PLATE_T - 1.0)
    .rect(FRAME_X, PLATE_Y)
    .extrude(FRAME_H + 1.0)
    .edges("|Z").fillet(FRAME_R)
)
body = plate.union(frame)

# ---------------- lid recess ----------------
recess = (
    cq.Workplane("XY")
    .workplane(offset=LEDGE_Z)
    .rect(RECESS_X, RECESS_Y)
    .extrude(RECESS_D + 1.0)
    .edges("|Z").fillet(RECESS_R)
)
body = body.cut(recess)

# ---------------- main pocket with corner bosses ----------------
pocket = (
    cq.Workplane("XY")
    .workplane(offset=FLOOR_T)
    .rect(POCKET_X, POCKET_Y)
    .extrude(LEDGE_Z - FLOOR_T + 0.01)
)
boss_pts = [(sx * BOSS_DX, sy * BOSS_DY) for sx in (-1, 1) for sy in (-1, 1)]
bosses = (
    cq.Workplane("XY")
    .workplane(offset=FLOOR_T - 0.5)
    .pushPoints(boss_pts)
    .circle(BOSS_R)
    .extrude(LEDGE_Z - FLOOR_T + 1.0)
)
pocket = pocket.cut(bosses)
body = body.cut(pocket)

# ---------------- vent slots through the floor ----------------
slot_pts = [(0.0, (i - (SLOT_N - 1) / 2.0) * SLOT_PITCH) for i in range(SLOT_N)]
slots = (
    cq.Workplane("XY")
    .workplane(offset=-1.0)
    .pushPoints(slot_pts)
    .rect(SLOT_L, SLOT_W)
    .extrude(FLOOR_T + 2.0)
)
body = body.cut(slots)

# ---------------- boss screw holes + hex nut traps (underside) ----------------
boss_holes = (
    cq.Workplane("XY")
    .workplane(offset=-1.0)
    .pushPoints(boss_pts)
    .circle(BOSS_HOLE_D / 2.0)
    .extrude(TOP + 2.0)
)
body = body.cut(boss_holes)
nuts = (
    cq.Workplane("XY")
    .workplane(offset=-1.0)
    .transformed(rotate=(0, 0, NUT_ROT))
    .pushPoints([
        (x * math.cos(math.radians(NUT_ROT)) + y * math.sin(math.radians(NUT_ROT)),
         -x * math.sin(math.radians(NUT_ROT)) + y * math.cos(math.radians(NUT_ROT)))
        for (x, y) in boss_pts
    ])
    .polygon(6, NUT_AF / 0.8660254)
    .extrude(NUT_DEPTH + 1.0)
)
body = body.cut(nuts)

# ---------------- flange holes: shallow top countersink + deep underside countersink ----------------

hole_pts = [
    (sx * HOLE_X, (j - (HOLE_N - 1) / 2.0) * HOLE_PITCH)
    for sx in (-1, 1)
    for j in range(HOLE_N)
]
r_h = HOLE_D / 2.0
top_depth = (TOP_CSK_D / 2.0 - r_h) / math.tan(math.radians(TOP_CSK_ANGLE / 2.0))
bot_depth = (CSK_D / 2.0 - r_h) / math.tan(math.radians(CSK_ANGLE / 2.0))
eps = 0.5


def hole_tool(x, y):
    cyl = cq.Solid.makeCylinder(r_h, PLATE_T + 2 * eps, cq.Vector(x, y, -eps))
    top_h = top_depth + eps
    top_cone = cq.Solid.makeCone(
        r_h,
        r_h + top_h * math.tan(math.radians(TOP_CSK_ANGLE / 2.0)),
        top_h,
        cq.Vector(x, y, PLATE_T - top_depth),
    )
    bot_h = bot_depth + eps
    bot_cone = cq.Solid.makeCone(
        r_h + bot_h * math.tan(math.radians(CSK_ANGLE / 2.0)),
        r_h,
        bot_h,
        cq.Vector(x, y, -eps),
    )
    return cyl.fuse(top_cone).fuse(bot_cone)


for (x, y) in hole_pts:
    body = body.cut(cq.Workplane("XY").add(hole_tool(x, y)))

result = body

VIEW = {"azimuth": 45, "elevation": 26}
